import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
T = 2.8            # plate / wall thickness
KEY = 18.0         # keycap base size
KEY_H = 4.0        # keycap height above its base slab
KEY_CH = 1.5       # chamfer on keycap top edges
BASE = 18.6        # key base slab size
BASE_H = 1.2       # key base slab height
HOLE = 14.0        # switch opening in the plate
SOCK = 17.0        # switch socket outer size (hangs under the plate)
SOCK_H = 2.5       # socket depth below the plate underside
SINK = 0.8         # key base sunk into the plate
POCKET = 11.0      # recess in the underside of each key base
POCKET_D = 1.2
PITCH = 19.5       # key pitch along the arc

COL_W = 22.5       # single finger column width
COL_W2 = 41.5      # double (index) column width

# finger column profile (local v = along column, +v = back ; z up)
R_COL = 60.0       # concave key arc radius
ZC_COL = 71.8      # height of key arc centre
B_DROP = 5.5       # middle column sits lower
TH_FRONT = -44.0   # ridge angle at the front (deg, from straight down)
TH_BACK = 17.8     # angle where the key arc meets the back lip
V_FRONT = -61.0    # front face foot
V_BACK = 27.4      # back face foot
RBK_COL = 30.0     # radius of the (slightly convex) back face
LIP_DV = 3.5       # back lip rise (along / up)
LIP_DZ = 2.6
RF_COL = 68.0      # front face radius
KEYS_COL = [-28.9, -10.3, 8.3]   # key angles on the arc

# thumb cluster profile
R_TH = 75.4
ZC_TH = 82.47
TH_T_FRONT = -48.6  # ridge (high end)
TH_T_BACK = 3.04    # low end: key arc meets the end lip
TH_LIP = ((1.0, 3.8), (2.6, 3.8))  # end lip: rise, then flat top (along / up)
TH_T_SLANT = 2.6    # run of the sloped end face
TH_T_WALL = 4.95    # where the outer thumb wall leaves the key arc
V_T_FRONT = -79.3   # front face foot
RF_TH = 55.0
KEYS_TH = [-6.2, -21.5, -37.0]


# ---------------------------------------------------------------- helpers
def _d(a, b):
    return math.hypot(a[0] - b[0], a[1] - b[1])


def arc_pt(c, r, th):
    """point on a key arc; th measured from straight down, + toward +v"""
    t = math.radians(th)
    return (c[0] + r * math.sin(t), c[1] - r * math.cos(t))


def circ_line(c, r, z, near):
    dz = z - c[1]
    du = math.sqrt(max(r * r - dz * dz, 0.0))
    s = [(c[0] + du, z), (c[0] - du, z)]
    return min(s, key=lambda p: _d(p, near))


def circ_circ(c1, r1, c2, r2, near):
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dy)
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    mx, my = c1[0] + a * dx / d, c1[1] + a * dy / d
    s = [(mx + h * dy / d, my - h * dx / d), (mx - h * dy / d, my + h * dx / d)]
    return min(s, key=lambda p: _d(p, near))


def line_circ(p, dvec, c, r, near):
    """intersection of line p + t*dvec with circle (c, r), closest to `near`"""
    fx, fy = p[0] - c[0], p[1] - c[1]
    a = dvec[0] ** 2 + dvec[1] ** 2
    b = 2 * (fx * dvec[0] + fy * dvec[1])
    cc = fx * fx + fy * fy - r * r
    disc = math.sqrt(max(b * b - 4 * a * cc, 0.0))
    s = [(p[0] + t * dvec[0], p[1] + t * dvec[1]) for t in ((-b + disc) / (2 * a), (-b - disc) / (2 * a))]
    return min(s, key=lambda q: _d(q, near))


def end_center(p0, p1, r, inward):
    """centre of a convex end arc through p0,p1 lying on the `inward` side"""
    mx, my = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    cx, cy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(cx, cy)
    nx, ny = -cy / L, cx / L
    if nx * inward[0] + ny * inward[1] < 0:
        nx, ny = -nx, -ny
    h = math.sqrt(max(r * r - (L / 2) ** 2, 0.0))
    return (mx + nx * h, my + ny * h)


def mid_on_circle(c, r, p, q):
    a1 = math.atan2(p[1] - c[1], p[0] - c[0])
    a2 = math.atan2(q[1] - c[1], q[0] - c[0])
    da = (a2 - a1 + math.pi) % (2 * math.pi) - math.pi
    a = a1 + da / 2
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def profile_solid(segs, width):
    """segs: list of ('l', p_end) or ('a', p_mid, p_end) starting at segs[0][1]"""
    wp = cq.Workplane("YZ").moveTo(*segs[0])
    for s in segs[1:]:
        if s[0] == "l":
            wp = wp.lineTo(*s[1])
        else:
            wp = wp.threePointArc(s[1], s[2])
    return wp.close().extrude(width / 2.0, both=True)


def key_solid(width_keys=1):
    """keycap(s) on a base slab, local: top normal +Z, plate surface at z=0 (base sunk SINK into it)"""
    k = None
    for i in range(width_keys):
        off = (i - (width_keys - 1) / 2.0) * PITCH
        base = (
            cq.Workplane("XY")
            .box(BASE, BASE, BASE_H + SINK, centered=(True, True, False))
            .translate((off, 0, -SINK))
        )
        cap = (
            cq.Workplane("XY")
            .box(KEY, KEY, KEY_H, centered=(True, True, False))
            .edges(">Z")
            .chamfer(KEY_CH)
            .translate((off, 0, BASE_H))
        )
        pocket = (
            cq.Workplane("XY")
            .box(POCKET, POCKET, POCKET_D + 0.01, centered=(True, True, False))
            .translate((off, 0, -SINK - 0.01))
        )
        one = base.union(cap).cut(pocket)
        k = one if k is None else k.union(one)
    return k


def socket_solid(width_keys=1):
    """square switch socket hanging under the plate (local: plate top at z=0)"""
    h = None
    for i in range(width_keys):
        off = (i - (width_keys - 1) / 2.0) * PITCH
        one = cq.Workplane("XY").box(SOCK, SOCK, SOCK_H + 1.2, centered=(True, True, False)).translate(
            (off, 0, -(T + SOCK_H))
        )
        h = one if h is None else h.union(one)
    return h


def hole_cutter(width_keys=1):
    """square switch openings through the plate and socket under each key"""
    h = None
    for i in range(width_keys):
        off = (i - (width_keys - 1) / 2.0) * PITCH
        one = cq.Workplane("XY").box(HOLE, HOLE, T + SOCK_H + 4, centered=(True, True, False)).translate(
            (off, 0, -(T + SOCK_H + 4) + 0.3)
        )
        h = one if h is None else h.union(one)
    return h


def place_key(k, c, r, th):
    """put a key (local, bottom at z=0) on the concave arc at angle th; arc in the YZ plane"""
    p = arc_pt(c, r, th)
    # key normal points to the arc centre: rotate about X by -th (tilt top toward -v for th<0)
    return k.rotate((0, 0, 0), (1, 0, 0), th).translate((0, p[0], p[1]))


def column(width, R, ZC, th_front, th_back, v_front, v_back, rf, key_angles, lip=(0.0, 0.0), rbk=0.0,
           width_keys=1, zbot=0.0, wall_l=False, wall_r=False, wall_nolip=False, th_wall_end=None):
    """One key column: a bent plate (convex front, concave key arc, lip + slanted back leg),
    optional side walls, open underneath.  Local frame: +Y = back, +Z = up, width along X."""
    c = (0.0, ZC)
    ridge = arc_pt(c, R, th_front)
    btop = arc_pt(c, R, th_back)
    f0 = (v_front, 0.0)
    cf = end_center(f0, ridge, rf, (1, 0))
    lips = [lip] if isinstance(lip[0], (int, float)) else list(lip)
    lip_pts = [(btop[0] + a, btop[1] + b) for a, b in lips if abs(a) + abs(b) > 1e-9]
    lip_pt = lip_pts[-1] if lip_pts else btop
    b0 = (v_back, 0.0)
    # ---- outer profile
    if zbot < 0:
        # extend the front face along its tangent and the back face along its slope below the ground
        tx, tz = f0[1] - cf[1], -(f0[0] - cf[0])
        if tz > 0:
            tx, tz = -tx, -tz
        f_ext = (f0[0] + tx * zbot / tz, zbot)
        segs = [f_ext, ("l", f0)]
    else:
        segs = [f0]
    segs.append(("a", mid_on_circle(cf, rf, f0, ridge), ridge))
    segs.append(("a", arc_pt(c, R, (th_front + th_back) / 2), btop))
    for p in lip_pts:
        segs.append(("l", p))
    if rbk > 0:
        cbk = end_center(b0, lip_pt, rbk, (-1, 0))
        segs.append(("a", mid_on_circle(cbk, rbk, lip_pt, b0), b0))
        tx, tz = b0[1] - cbk[1], -(b0[0] - cbk[0])
    else:
        segs.append(("l", b0))
        tx, tz = b0[0] - lip_pt[0], b0[1] - lip_pt[1]
    if zbot < 0:
        if tz > 0:
            tx, tz = -tx, -tz
        segs.append(("l", (b0[0] + tx * zbot / tz, zbot)))
    outer = profile_solid(segs, width)

    # ---- inner cavity (offset by T, open at the bottom)
    zc_ = min(zbot, 0.0) - 1.0
    Ri = R + T
    i_ridge = circ_circ(cf, rf - T, c, Ri, ridge)
    i_f0 = circ_line(cf, rf - T, zc_, (f0[0] + T, zc_))
    if rbk > 0:
        i_btop = circ_circ(cbk, rbk - T, c, Ri, btop)
        i_b0 = circ_line(cbk, rbk - T, zc_, (b0[0] - T, zc_))
        back_seg = ("a", mid_on_circle(cbk, rbk - T, i_btop, i_b0), i_b0)
    else:
        dv = (b0[0] - lip_pt[0], b0[1] - lip_pt[1])
        L = math.hypot(*dv)
        nrm = (-dv[1] / L, dv[0] / L)
        if nrm[0] > 0:
            nrm = (-nrm[0], -nrm[1])
        q = (lip_pt[0] + nrm[0] * T, lip_pt[1] + nrm[1] * T)
        i_btop = line_circ(q, dv, c, Ri, btop)
        t = (zc_ - q[1]) / dv[1]
        i_b0 = (q[0] + t * dv[0], zc_)
        back_seg = ("l", i_b0)
    th_i = math.degrees(math.atan2(i_btop[0] - c[0], c[1] - i_btop[1]))
    isegs = [i_f0, ("a", mid_on_circle(cf, rf - T, i_f0, i_ridge), i_ridge),
             ("a", arc_pt(c, Ri, (th_front + th_i) / 2), i_btop), back_seg]
    sep = wall_nolip  # walls built separately (they stop below the end lip)
    x0 = -width / 2.0 + T if (wall_l and not sep) else -width / 2.0 - 1.0
    x1 = width / 2.0 - T if (wall_r and not sep) else width / 2.0 + 1.0
    inner = profile_solid(isegs, x1 - x0).translate(((x0 + x1) / 2.0, 0, 0))
    body = outer.cut(inner)
    if sep:
        twe = th_back if th_wall_end is None else th_wall_end
        wsegs = [f0, ("a", mid_on_circle(cf, rf, f0, ridge), ridge),
                 ("a", arc_pt(c, R, (th_front + twe) / 2), arc_pt(c, R, twe)), ("l", b0)]
        for on, xs in ((wall_l, -1), (wall_r, 1)):
            if on:
                w = profile_solid(wsegs, T).translate((xs * (width - T) / 2.0, 0, 0))
                body = body.union(w)

    # ---- switch sockets and openings, then keys
    sk = socket_solid(width_keys)
    hc = hole_cutter(width_keys)
    for th in key_angles:
        body = body.union(place_key(sk, c, R, th))
    for th in key_angles:
        body = body.cut(place_key(hc, c, R, th))
    k = key_solid(width_keys)
    for th in key_angles:
        body = body.union(place_key(k, c, R, th))
    return body


def place(obj, rot, x, y, z=0.0, tent=0.0):
    o = obj
    if tent:
        o = o.rotate((0, 0, 0), (0, 1, 0), tent)
    return o.rotate((0, 0, 0), (0, 0, 1), rot).translate((x, y, z))


# ---------------------------------------------------------------- build
col_args = dict(R=R_COL, th_front=TH_FRONT, th_back=TH_BACK, v_front=V_FRONT,
                v_back=V_BACK, rf=RF_COL, key_angles=KEYS_COL, lip=(LIP_DV, LIP_DZ), rbk=RBK_COL)

single = column(COL_W, ZC=ZC_COL, **col_args)
colB = place(column(COL_W, ZC=ZC_COL - B_DROP, **col_args), 0.0, 5.6, 40.5)
colC = place(single, -3.5, 28.2, 29.7)
colD = place(column(COL_W, ZC=ZC_COL, wall_r=True, **col_args), -14.0, 53.3, 10.8)

A_TENT = 10.0
A_RAISE = 6.6
A_BACK_TRIM = -1.0
A_PITCH = 1.3      # index column tipped up toward the back about its front ridge
dbl = column(COL_W2, ZC=ZC_COL, zbot=-15.0, width_keys=2, **dict(col_args, v_back=V_BACK - A_BACK_TRIM))
ridgeA = arc_pt((0.0, ZC_COL), R_COL, TH_FRONT)
dbl = dbl.rotate((0, ridgeA[0], ridgeA[1]), (1, ridgeA[0], ridgeA[1]), A_PITCH)
colA = place(dbl, 4.0, -31.2, 31.3, A_RAISE, A_TENT)

# thumb cluster: same construction, low end = "back", high ridge = "front"
th_back_v = math.sin(math.radians(TH_T_BACK)) * R_TH
thumb = column(COL_W, R=R_TH, ZC=ZC_TH, th_front=TH_T_FRONT, th_back=TH_T_BACK, v_front=V_T_FRONT,
               v_back=th_back_v + TH_LIP[-1][0] + TH_T_SLANT, rf=RF_TH, key_angles=KEYS_TH, lip=TH_LIP,
               wall_l=True, wall_r=False, wall_nolip=True, th_wall_end=TH_T_WALL)
TH_ROT = 119.4
TH_CENTRE = (-57.6, -53.3)           # plan position of the thumb key-arc centre
thumbP = place(thumb, TH_ROT, TH_CENTRE[0], TH_CENTRE[1])

result = colA.union(colB).union(colC).union(colD).union(thumbP)
result = result.intersect(cq.Workplane("XY").box(400, 400, 200, centered=(True, True, False)))
